import math
import cadquery as cq

# =====================================================================
#  Shielded connector: rounded sheet-metal shell with a layered plastic
#  insert running through it (front opening with slot / tongue), lower
#  latch tray, side straps and a rear plate.
#  X = width, Y = depth (front of the insert at Y = 0), Z = height.
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
W = 12.98          # overall width (X)
H = 10.0           # overall height (Z)
HW = W / 2.0
R_OUT = 1.6        # shell edge radius (edges along Y and at the back)
R_FR = 1.85        # radius of the rounded front edges of the shell
T_SH = 0.35        # sheet thickness of the top cover
Y_FACE = 0.63      # flat front face of the shell
Y_BACK = 9.68      # back face of the shell
Y_FR = 2.6         # depth of the front detail zone

# insert (plastic housing) that runs through the shell
INS_HW = 5.67
INS_Z0, INS_Z1 = 2.07, 7.90
INS_L1, INS_L2 = 3.33, 5.81     # layer lines of the stacked housing
BLK_HW = 3.13                   # half width of the central opening
TNG_Z1 = 4.36                   # top of the tongue bar (bottom = INS_L1)
TOP_Z0 = 5.24                   # underside of the top slab in the middle
SLB_X0, SLB_X1 = -1.82, 2.18    # shallow part of the upper slot
KEY_X0, KEY_X1 = -0.82, 1.20    # polarising key way in the lower opening
Y_POCK = 3.0                    # depth of the central opening

# front of the shell
Y_LIP = 0.74        # top lip front
Y_TRAY = 0.33       # lower tray front
Z_FLOOR = 0.79      # floor of the lower opening
Z_TRAY = 2.27       # lower tray side wall height at front
Z_FLANGE = 7.28     # bottom edge of the top cover side flange

# back plate / straps
BP_Y0, BP_Y1 = 9.46, 10.05
ST_Z0, ST_Z1 = 5.92, Z_FLANGE
ST_Y0, ST_Y1 = 6.60, 9.36

# seams between the sheet-metal parts
S1_PTS = [(0.88, 2.29), (1.30, 2.42), (1.80, 2.83), (2.20, 3.33), (2.60, 4.11),
          (3.04, 4.99), (3.34, 5.59), (3.56, 5.83), (3.875, ST_Z0), (4.40, ST_Z0)]   # upper edge of the tray side (Y, Z)
Y_SEAM_TOP = 3.42     # top cover seam
Y_SEAM_BOT = 3.04     # lower tray seam


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


def rr_prism(hw, z0, z1, r, y0, y1):
    """rounded rectangle (in XZ) extruded along Y"""
    return box(-hw, hw, y0, y1, z0, z1).edges("|Y").fillet(r)


def yz_prism(pts, x0, x1):
    return (cq.Workplane("YZ", origin=(x0, 0, 0))
            .polyline(pts).close().extrude(x1 - x0))


# ---------------- main shell body ----------------
body = box(-HW, HW, Y_FACE, Y_BACK, 0, H)
body = body.faces("<Y").edges().fillet(R_FR)
body = body.edges("|Y").fillet(R_OUT)
body = body.faces(">Y").edges().fillet(R_OUT - 0.01)

OUT = rr_prism(HW, 0, H, R_OUT, 0.0, Y_FR)
INN = rr_prism(HW - T_SH, T_SH, H - T_SH, R_OUT - T_SH, -0.1, Y_FR + 0.1)

# top cover front: lip + side flanges with chevron ends
chev = [(1.11, Z_FLANGE), (1.11, 8.09), (1.48, 8.62), (Y_LIP, 9.67),
        (Y_LIP, H + 0.1), (Y_FR, H + 0.1), (Y_FR, Z_FLANGE)]
cover = OUT.cut(INN).intersect(yz_prism(chev, -HW - 1, HW + 1))

# trapezoidal notch in the lip
notch = (cq.Workplane("XY", origin=(0, 0, H - T_SH - 0.05))
         .polyline([(-2.34, Y_LIP - 0.1), (2.34, Y_LIP - 0.1),
                    (1.67, 1.41), (-1.67, 1.41)]).close()
         .extrude(T_SH + 0.2))
cover = cover.cut(notch)

# lower tray: floor + side walls with chamfered tops
floor_ = box(-HW, HW, Y_TRAY, Y_FR, 0, Z_FLOOR)


def tray_side(x0, x1):
    """side wall of the lower tray: chamfered front, S-shaped upper edge"""
    return (cq.Workplane("YZ", origin=(x0, 0, 0))
            .moveTo(Y_TRAY, Z_FLOOR - 0.01)
            .lineTo(Y_TRAY, 1.90)
            .lineTo(Y_LIP, Z_TRAY)
            .lineTo(*S1_PTS[0])
            .spline(S1_PTS[1:], tangents=[(1, 0.3), (1, 0)], includeCurrent=True)
            .lineTo(S1_PTS[-1][0], Z_FLOOR - 0.01)
            .close()
            .extrude(x1 - x0))


tray_w = tray_side(-HW, -INS_HW).union(tray_side(INS_HW, HW))
tray = floor_.union(tray_w).intersect(rr_prism(HW, 0, H, R_OUT, 0.0, 5.0))

# windows with latch ramps in the tray front
for sd in (-1, 1):
    xa, xb = sorted((sd * 2.44, sd * 4.50))
    tray = tray.cut(box(xa, xb, Y_TRAY - 0.1, Y_TRAY + 0.45, 0.16, 0.68))
    ramp = yz_prism([(Y_TRAY + 0.45, 0.16), (Y_TRAY + 0.05, 0.16),
                     (Y_TRAY + 0.45, 0.55)], xa + 0.05, xb - 0.05)
    tray = tray.union(ramp)

# ---------------- insert ----------------
ins = box(-INS_HW, INS_HW, 0.0, Y_FR, INS_Z0, INS_Z1)

# ---------------- assemble ----------------
part = body.union(cover).union(tray).union(ins)

# arched clearance notches of the shell front opening above / below the insert
def arch(z_base, dz):
    """arch-shaped XZ profile sitting on z_base, height dz (sign = direction)"""
    rc = (ARCH_X1 - ARCH_X0) ** 2 / (2 * abs(dz)) + abs(dz) / 2
    sg = 1 if dz > 0 else -1
    zc = z_base + dz - sg * rc
    mid = lambda x: zc + sg * math.sqrt(rc ** 2 - (x - ARCH_X0) ** 2)
    xm = (ARCH_X0 + ARCH_X1) / 2
    wp = (cq.Workplane("XZ", origin=(0, 0.5, 0))
          .moveTo(-ARCH_X1, z_base)
          .threePointArc((-xm, mid(xm)), (-ARCH_X0, z_base + dz))
          .lineTo(ARCH_X0, z_base + dz)
          .threePointArc((xm, mid(xm)), (ARCH_X1, z_base))
          .close())
    return wp.extrude(-(ARCH_D - 0.5))


ARCH_X0, ARCH_X1 = 2.37, 3.34   # flat part / foot of the arches (half widths)
ARCH_D = 0.95                   # depth of the notches (Y)
part = part.cut(arch(INS_Z1, 0.28)).cut(arch(INS_Z0, -0.21))

# central opening of the insert: upper slot, tongue, lower opening with step
part = part.cut(box(-BLK_HW, BLK_HW, -0.1, Y_POCK, INS_Z0, TOP_Z0))
part = part.union(box(-BLK_HW, BLK_HW, 0.0, Y_POCK + 0.1, INS_L1, TNG_Z1))
part = part.union(box(SLB_X0, SLB_X1, 0.70, Y_POCK + 0.1, TNG_Z1 - 0.01, TOP_Z0))
step = box(-BLK_HW, BLK_HW, 0.45, Y_POCK + 0.1, INS_Z0, 2.90)
step = step.faces(">Z").edges("<Y").fillet(0.70)
part = part.union(step)
part = part.cut(box(KEY_X0, KEY_X1, 1.60, Y_POCK + 0.4, INS_Z0 + 0.03, INS_L1))

# ---------------- back plate (rear end of the insert) ----------------
part = part.union(box(-INS_HW, INS_HW, BP_Y0, BP_Y1, INS_Z0 - 0.01, INS_Z1 + 0.02))

# ---------------- side straps ----------------
for sd in (-1, 1):
    x0, x1 = (HW - 0.30, HW) if sd > 0 else (-HW, -HW + 0.30)
    st = box(x0, x1, ST_Y0, ST_Y1, ST_Z0, ST_Z1)
    st = st.edges("|X").edges(">Y").fillet(0.3)
    part = part.union(st)

# small dimple on the top
part = part.cut(cq.Workplane("XY", origin=(0, 3.86, H - 0.1)).circle(0.16).extrude(0.2))

shp = part.val()

# ---------------- seam lines of the sheet-metal parts ----------------
# Imprinted on the existing faces: they split faces along the seams of
# the assembled sheet-metal parts without changing the shape.
V = cq.Vector
YF = Y_FACE + R_FR          # start of the flat side face (behind the front radius)
YB = Y_BACK - R_OUT         # end of the flat side face (before the back radius)
XC = HW - R_OUT             # axis of the edge radii along Y


def face_at(shape, p, tol=1e-3):
    v = cq.Vertex.makeVertex(*p)
    best = min(shape.Faces(), key=lambda f: f.distance(v))
    return best if best.distance(v) < tol else None


def pl(pts):
    return [cq.Edge.makeLine(V(*a), V(*b)) for a, b in zip(pts[:-1], pts[1:])]


def side_edges(sd):
    X = sd * HW
    c45 = math.cos(math.pi / 4)
    E = []

    def P(y, z):
        return V(X, y, z)

    # bottom edge of the top cover flange / top edge of the strap
    E.append(cq.Edge.makeLine(P(YF - 0.1, ST_Z1), P(YB + 0.1, ST_Z1)))
    # rounded end of the front side panel
    r, y0 = 0.42, 6.25
    E.append(cq.Edge.makeThreePointArc(P(y0, ST_Z1), P(y0 + r * c45, ST_Z1 - r + r * c45),
                                       P(y0 + r, ST_Z1 - r)))
    E.append(cq.Edge.makeLine(P(y0 + r, ST_Z1 - r), P(y0 + r, ST_Z0 + r)))
    E.append(cq.Edge.makeThreePointArc(P(y0 + r, ST_Z0 + r), P(y0 + r * c45, ST_Z0 + r - r * c45),
                                       P(y0, ST_Z0)))
    # bottom edge of the strap / side panel
    E.append(cq.Edge.makeLine(P(4.40, ST_Z0), P(YB + 0.1, ST_Z0)))
    # S-shaped upper edge of the tray side (where it is flush with the shell side)
    # (the very edge of the tray side solid is reused, so it matches exactly)
    E += [e for e in tray_w.edges("%BSPLINE").vals()
          if abs(e.Center().x - X) < 1e-3]
    # S-shaped edge of the lower tray side
    E.append(cq.Edge.makeSpline([P(6.60, ST_Z0), P(6.20, 5.62), P(5.36, 4.07), P(4.59, 2.83),
                                 P(4.05, 2.36), P(3.51, 2.29)],
                                tangents=[V(0, -1, 0), V(0, -1, 0)]))
    E += pl([(X, 3.51, 2.29), (X, Y_SEAM_BOT, 1.98), (X, Y_SEAM_BOT, R_OUT - 0.05)])
    E.append(cq.Edge.makeThreePointArc(
        V(X, Y_SEAM_BOT, R_OUT),
        V(sd * (XC + R_OUT * c45), Y_SEAM_BOT, R_OUT - R_OUT * c45),
        V(sd * XC, Y_SEAM_BOT, 0)))
    # zigzag seam of the top cover on the side
    E += pl([(X, 4.06, 8.45), (X, 3.81, 8.09), (X, 3.81, 7.46), (X, 3.97, ST_Z1)])
    # ... and over the top edge radius (projected onto it)
    tf = face_at(shp, (sd * (XC + R_OUT * c45), 5.0, H - R_OUT + R_OUT * c45))
    if tf is not None:
        o = 1.5
        a = V(sd * (XC + o), Y_SEAM_TOP, H + o)
        b = V(sd * (HW + o), 4.06, H - R_OUT + o)
        ln = cq.Edge.makeLine(a + (a - b) * 0.03, b + (b - a) * 0.03)
        E.append(ln.project(tf, V(-sd, 0, -1)))
    return E


edges = side_edges(1) + side_edges(-1)
# top cover seam with its trapezoidal tongue
edges += pl([(-XC - 0.1, Y_SEAM_TOP, H), (-2.34, Y_SEAM_TOP, H), (-1.67, 4.07, H),
             (1.67, 4.07, H), (2.34, Y_SEAM_TOP, H), (XC + 0.1, Y_SEAM_TOP, H)])
# lower tray seam on the bottom
edges.append(cq.Edge.makeLine(V(-XC - 0.1, Y_SEAM_BOT, 0), V(XC + 0.1, Y_SEAM_BOT, 0)))
# layers of the insert (front face, side faces, rear plate)
for sd in (-1, 1):
    edges += pl([(sd * (INS_HW + 0.1), 0, INS_L2), (sd * BLK_HW, 0, INS_L2),
                 (sd * BLK_HW, 0, TOP_Z0 - 0.05)])
    edges.append(cq.Edge.makeLine(V(sd * (INS_HW + 0.1), 0, INS_L1),
                                  V(sd * (BLK_HW - 0.05), 0, INS_L1)))
    edges.append(cq.Edge.makeLine(V(sd * BLK_HW, 0, INS_L1 - 0.05),
                                  V(sd * BLK_HW, 0, TNG_Z1 + 0.05)))
    for z in (INS_L1, INS_L2):
        edges.append(cq.Edge.makeLine(V(sd * INS_HW, -0.1, z), V(sd * INS_HW, 1.3, z)))
    for z in (3.31, 5.83):
        edges.append(cq.Edge.makeLine(V(sd * INS_HW, BP_Y0 - 0.1, z), V(sd * INS_HW, BP_Y1 + 0.1, z)))
edges += pl([(INS_HW + 0.1, BP_Y1, 5.83), (1.02, BP_Y1, 5.83), (1.02, BP_Y1, 4.91),
             (-0.61, BP_Y1, 4.91), (-0.61, BP_Y1, 5.83), (-INS_HW - 0.1, BP_Y1, 5.83)])
edges.append(cq.Edge.makeLine(V(-INS_HW - 0.1, BP_Y1, 3.31), V(INS_HW + 0.1, BP_Y1, 3.31)))

try:
    pieces = shp.split(*edges).Solids()
    result = max(pieces, key=lambda so: so.Volume()) if pieces else shp
    if not result.isValid():
        result = shp
except Exception:
    result = shp
